import math

import cadquery as cq

# =====================================================================
#  Fan enclosure: open-top box with a lid tongue, screw bosses,
#  recessed side windows and two 40 mm fan openings in the floor.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # outer length (X)
W = 60.0           # outer width  (Y)
H_BODY = 58.0      # height of the outer wall (outer ledge level)
LIP_H = 2.0        # height of the lid tongue above the body
R_OUT = 4.5        # outer vertical corner radius
R_BOT = 1.8        # fillet on the bottom perimeter edges
R_IN = 1.0         # inner vertical corner radius of the cavity

T_WALL = 4.0       # side wall thickness
T_FLOOR = 4.0      # floor thickness

LIP_IN0 = 1.9      # tongue outer face inset from the body outer face
LIP_W = 2.1        # tongue width (inner face flush with the wall)

SHELF_IN = 7.0     # inner edge inset of the top shelf (= screw boss centre inset)
SHELF_T = 2.0      # shelf thickness
SHELF_FIL = 1.5    # concave fillet where the bosses meet the shelf edge

BOSS_R = 4.0       # screw boss radius
BOSS_H = 5.0       # screw boss length (hanging from the top)
BOSS_HOLE_D = 3.7  # screw hole diameter
WEB_SPREAD = 5.2   # how far the boss web foot reaches along the wall from the boss centre line

# side windows (front and back walls)
WIN_W = 62.2
WIN_H = 43.2
WIN_ZC = 30.8
WIN_R = 12.0
REC_OFF = 2.8      # recess frame offset around the window
REC_D = 1.9        # recess depth

# fan openings in the floor
FAN_X = 23.85      # fan centres at +-FAN_X
FAN_D = 36.5       # through bore
FAN_CB_D = 39.9    # top counterbore
FAN_CB_DEPTH = 1.0
FAN_BCB_D = 39.0   # bottom counterbore
FAN_BCB_DEPTH = 1.0
FAN_PITCH_X = 32.0 # fan screw pattern
FAN_PITCH_Y = 31.2
FAN_SCREW_D = 2.8

# snap catches on the tongue
BUMP_L = 5.0       # length along the wall
BUMP_P = 0.45      # protrusion
BUMP_Z0 = 0.6      # bottom of the catch above the outer ledge
BUMP_Z1 = 1.4      # top of the catch above the outer ledge
BUMP_X = 15.0      # catch positions on the long sides (+-X)

# derived levels
Z_SHELF = H_BODY - SHELF_T
Z_BOSS = H_BODY - BOSS_H
HX = L / 2 - SHELF_IN
HY = W / 2 - SHELF_IN
BOSS_PTS = [(sx * HX, sy * HY) for sx in (-1, 1) for sy in (-1, 1)] + [(0.0, HY), (0.0, -HY)]


def slab(z0, h, sketch):
    """Extrude a sketch from height z0 by h."""
    return cq.Workplane("XY").workplane(offset=z0).placeSketch(sketch).extrude(h)


def rrect(w, h, r):
    return cq.Sketch().rect(w, h).vertices().fillet(r)


# ---------------- main body ----------------
body = slab(0, H_BODY, rrect(L, W, R_OUT))
body = body.faces("<Z").edges().fillet(R_BOT)

# cavity below the shelf
body = body.cut(slab(T_FLOOR, Z_SHELF - T_FLOOR, rrect(L - 2 * T_WALL, W - 2 * T_WALL, R_IN)))

# opening through the top shelf, leaving the round screw boss heads
shelf_open = (
    cq.Sketch()
    .rect(L - 2 * SHELF_IN, W - 2 * SHELF_IN)
    .push(BOSS_PTS)
    .circle(BOSS_R, mode="s")
    .reset()
    .vertices()
    .fillet(SHELF_FIL)
)
body = body.cut(slab(Z_SHELF - 0.01, SHELF_T + 1.0, shelf_open))

# ---------------- screw bosses below the shelf ----------------

def tangent_point(P, C, r, Q):
    """Tangent point on circle (C, r) seen from external point P; of the two, the one farther from Q."""
    dx, dy = P[0] - C[0], P[1] - C[1]
    d = math.hypot(dx, dy)
    th = math.acos(r / d)
    a0 = math.atan2(dy, dx)
    cands = [(C[0] + r * math.cos(a0 + s_ * th), C[1] + r * math.sin(a0 + s_ * th)) for s_ in (1, -1)]
    return max(cands, key=lambda t: math.hypot(t[0] - Q[0], t[1] - Q[1]))


def boss_web(C, P1, P2, Q, back):
    """Boss body below the shelf: hull of the boss circle and two foot points P1, P2 on the wall(s),
    closed through 'back' points buried in the wall."""
    T1 = tangent_point(P1, C, BOSS_R, Q)
    T2 = tangent_point(P2, C, BOSS_R, Q)
    h = Z_SHELF - Z_BOSS
    web = (
        cq.Workplane("XY").workplane(offset=Z_BOSS)
        .polyline([P1, T1, C, T2, P2] + list(back)).close()
        .extrude(h)
    )
    cyl = cq.Workplane("XY").workplane(offset=Z_BOSS).center(*C).circle(BOSS_R).extrude(h + 0.2)
    return cyl.union(web)


IX = L / 2 - T_WALL          # inner wall faces
IY = W / 2 - T_WALL
E = 0.3                      # burial into the wall
for (px, py) in BOSS_PTS:
    sy = 1.0 if py > 0 else -1.0
    C = (px, py)
    if px == 0:
        P1 = (-WEB_SPREAD, sy * IY)
        P2 = (WEB_SPREAD, sy * IY)
        Q = (0.0, sy * (IY + 10.0))
        back = [(WEB_SPREAD, sy * (IY + E)), (-WEB_SPREAD, sy * (IY + E))]
    else:
        sx = 1.0 if px > 0 else -1.0
        K = (sx * IX, sy * IY)                       # inner corner
        P1 = (sx * IX, py - sy * WEB_SPREAD)          # foot on the end wall
        P2 = (px - sx * WEB_SPREAD, sy * IY)          # foot on the long wall
        Q = (K[0] + sx * 10.0, K[1] + sy * 10.0)
        back = [(P2[0], sy * (IY + E)), (sx * (IX + E), sy * (IY + E)), (sx * (IX + E), P1[1])]
    body = body.union(boss_web(C, P1, P2, Q, back))

# screw holes through the bosses
holes = (
    cq.Workplane("XY").workplane(offset=Z_BOSS - 0.5)
    .pushPoints(BOSS_PTS).circle(BOSS_HOLE_D / 2).extrude(BOSS_H + LIP_H + 2)
)
body = body.cut(holes)

# ---------------- lid tongue ----------------
lip = slab(H_BODY, LIP_H, rrect(L - 2 * LIP_IN0, W - 2 * LIP_IN0, R_OUT - LIP_IN0))
lip = lip.cut(
    slab(H_BODY - 0.01, LIP_H + 1,
         rrect(L - 2 * (LIP_IN0 + LIP_W), W - 2 * (LIP_IN0 + LIP_W),
               max(R_OUT - LIP_IN0 - LIP_W, 0.3)))
)
body = body.union(lip)

# snap catches: small ridged pads (triangular section, rounded ends) standing proud of
# the tongue's outer faces
zc = H_BODY + (BUMP_Z0 + BUMP_Z1) / 2
bh = BUMP_Z1 - BUMP_Z0


def catch():
    # built for the +Y face; outward = +Y
    ridge = (
        cq.Workplane("YZ")
        .polyline([(-0.3, zc - bh / 2), (0.0, zc - bh / 2), (BUMP_P, zc), (0.0, zc + bh / 2), (-0.3, zc + bh / 2)])
        .close()
        .extrude(BUMP_L / 2, both=True)
    )
    ends = (
        cq.Workplane("XZ", origin=(0, 0, zc))
        .slot2D(BUMP_L, bh)
        .extrude(-(BUMP_P + 0.6))
        .translate((0, -0.4, 0))
    )
    return ridge.intersect(ends)


for bx in (-BUMP_X, BUMP_X):
    for s in (-1, 1):
        c = catch().rotate((0, 0, 0), (0, 0, 1), 0 if s > 0 else 180)
        body = body.union(c.translate((bx, s * (W / 2 - LIP_IN0), 0)))
for s in (-1, 1):
    c = catch().rotate((0, 0, 0), (0, 0, 1), -90 if s > 0 else 90)
    body = body.union(c.translate((s * (L / 2 - LIP_IN0), 0, 0)))

# ---------------- side windows with recessed frame ----------------
for s in (-1, 1):
    yf = s * W / 2
    win = (
        cq.Workplane("XZ", origin=(0, yf, WIN_ZC))
        .placeSketch(rrect(WIN_W, WIN_H, WIN_R))
        .extrude(T_WALL + 3.0, both=True)
    )
    body = body.cut(win)
    rec = (
        cq.Workplane("XZ", origin=(0, yf, WIN_ZC))
        .placeSketch(rrect(WIN_W + 2 * REC_OFF, WIN_H + 2 * REC_OFF, WIN_R + REC_OFF))
        .extrude(REC_D, both=True)
    )
    body = body.cut(rec)

# ---------------- fan openings in the floor ----------------
fan_pts = [(-FAN_X, 0.0), (FAN_X, 0.0)]
bore = cq.Workplane("XY").workplane(offset=-1).pushPoints(fan_pts).circle(FAN_D / 2).extrude(T_FLOOR + 2)
body = body.cut(bore)
cb = (
    cq.Workplane("XY").workplane(offset=T_FLOOR - FAN_CB_DEPTH)
    .pushPoints(fan_pts).circle(FAN_CB_D / 2).extrude(FAN_CB_DEPTH + 1)
)
body = body.cut(cb)
bcb = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints(fan_pts).circle(FAN_BCB_D / 2).extrude(FAN_BCB_DEPTH + 1)
)
body = body.cut(bcb)

scr_pts = [
    (fx + dx, fy + dy)
    for fx, fy in fan_pts
    for dx in (-FAN_PITCH_X / 2, FAN_PITCH_X / 2)
    for dy in (-FAN_PITCH_Y / 2, FAN_PITCH_Y / 2)
]
scr = cq.Workplane("XY").workplane(offset=-1).pushPoints(scr_pts).circle(FAN_SCREW_D / 2).extrude(T_FLOOR + 2)
body = body.cut(scr)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
